import cadquery as cq

# ---- driving dimensions (mm) ----
P = 12.7            # hole pitch (1/2 inch system)
N_LONG = 10         # holes along the length
N_VERT = 3          # hole rows in the upright leg
N_HORZ = 2          # hole rows in the flat leg
T = 1.3             # sheet thickness
EDGE = 0.5 * P      # hole centre to free edge / to inner face of the other leg
HOLE_D = 0.40 * P   # hole diameter
R_CORNER = 0.5 * P  # free-corner radius (concentric with the corner holes)

L = N_LONG * P                            # overall length (Y)
H = T + EDGE + (N_VERT - 1) * P + EDGE    # overall height of upright leg (Z)
W = T + EDGE + (N_HORZ - 1) * P + EDGE    # overall width of flat leg (X)

# ---- upright leg: plate in the YZ plane, thickness along +X, top corners rounded ----
upright = (
    cq.Workplane("XY")
    .box(T, L, H, centered=(False, True, False))
    .edges("|X and >Z")
    .fillet(R_CORNER)
)

# ---- flat leg: plate in the XY plane, thickness along +Z, outer corners rounded ----
flat = (
    cq.Workplane("XY")
    .box(W, L, T, centered=(False, True, False))
    .edges("|Z and >X")
    .fillet(R_CORNER)
)

body = upright.union(flat)


def hole_cutter(centres, normal, seam_dir, depth):
    """Through-hole cylinders at global centres (on the start plane), axis along normal.
    seam_dir only chooses where the cylinder seam lies (cosmetic)."""
    n = cq.Vector(*normal).normalized()
    x = cq.Vector(*seam_dir)
    x = (x - n * x.dot(n)).normalized()
    y = n.cross(x)
    o = cq.Vector(*centres[0])
    pl = cq.Plane(origin=o.toTuple(), xDir=x.toTuple(), normal=n.toTuple())
    local = [((cq.Vector(*c) - o).dot(x), (cq.Vector(*c) - o).dot(y)) for c in centres]
    return cq.Workplane(pl).pushPoints(local).circle(HOLE_D / 2).extrude(depth)


ys = [-L / 2 + EDGE + i * P for i in range(N_LONG)]

# upright holes: axis along X, 3 rows x 10
zs = [H - EDGE - j * P for j in range(N_VERT)]
cut_v = hole_cutter([(-T, y, z) for y in ys for z in zs], (1, 0, 0), (0, -1, 1), 3 * T)

# flat-leg holes: axis along Z, 2 rows x 10
xs = [W - EDGE - k * P for k in range(N_HORZ)]
cut_h = hole_cutter([(x, y, -T) for x in xs for y in ys], (0, 0, 1), (1, 1, 0), 3 * T)

result = body.cut(cut_v).cut(cut_h)

VIEW = {"azimuth": 45, "elevation": 26}
